import cadquery as cq
import math

# ---------------------------------------------------------------
# "Sphere-cube" frame: a ball trimmed by a cube (six flat round
# faces) with three orthogonal through-bores, one per face pair.
# The bores meet in the middle, leaving eight spherical-triangle
# corners joined by twelve slender arched webs.
# ---------------------------------------------------------------

# Driving dimensions (mm)
CUBE = 30.0          # cube edge length (flat-to-flat distance)
SPHERE_DIA = 40.0    # diameter of the ball the cube is cut from
BORE_DIA = 22.6      # diameter of the three orthogonal through-bores

A = CUBE / 2.0
SPHERE_R = SPHERE_DIA / 2.0
BORE_R = BORE_DIA / 2.0
FLAT_R = math.sqrt(SPHERE_R ** 2 - A ** 2)   # radius of each flat face
BORE_LEN = 2.0 * SPHERE_DIA                  # long enough to go clean through
assert BORE_R < FLAT_R < A < SPHERE_R

# Ball. The primitive is turned so its poles sit in the X bores and its
# seam meridian runs through the +Y bore (keeps the seam line out of sight).
ball = (cq.Workplane("XY").sphere(SPHERE_R)
        .rotate((0, 0, 0), (1, 1, 1), 120))

# Trim to the cube -> six flat circular faces
cube = cq.Workplane("XY").box(CUBE, CUBE, CUBE)
body = ball.intersect(cube)

# Three orthogonal through-bores (cylinder seams turned to hidden spots)
bore_z = (cq.Workplane("XY").circle(BORE_R).extrude(BORE_LEN, both=True)
          .rotate((0, 0, 0), (0, 0, 1), 225))
bore_x = (cq.Workplane("YZ").circle(BORE_R).extrude(BORE_LEN, both=True)
          .rotate((0, 0, 0), (1, 0, 0), 180))
bore_y = cq.Workplane("XZ").circle(BORE_R).extrude(BORE_LEN, both=True)

result = body.cut(bore_z).cut(bore_x).cut(bore_y)

VIEW = {"azimuth": 45, "elevation": 26}
